import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
from OCP.TColgp import TColgp_Array1OfPnt2d
from OCP.gp import gp_Pnt2d

# ---------------- driving dimensions ----------------
# All sizes are given in drawing units and multiplied by K (mm per unit).
K = 0.6

# finger pad: egg shaped outline in XZ (front face at Y=0), thickness along +Y
PAD_T = 30.8            # mean thickness
PAD_TOP = 70.6          # top of pad above the shaft axis
PAD_BOT = -25.6         # bottom of pad
PAD_BACK_TILT = 3.5     # back face leans forward: bottom thicker than top by this
PAD_RT = 26.35          # radius of the upper (wide) end
PAD_XT = -2.3           # X offset of the upper end
PAD_RB = 23.0           # radius of the lower end
PAD_XB = 0.5            # X offset of the lower end
PAD_R_TOP = 15.0 / K    # back rounding radius at the top (variable fillet)
PAD_R_SHOULDER = 0.8    # how far the large top radius extends along the top arc
PAD_R_SIDE = 8.0 / K    # back rounding radius at the sides
PAD_R_LOW = 6.0 / K     # back rounding radius at the lower ends of the sides
PAD_R_BOT = 3.0 / K     # back rounding radius at the bottom centre
PAD_R_FRONT = 1.5 / K   # rounding of the front face edge

# tapered shaft (loft between two oval sections)
SH_SECTIONS = [  # (Y, half-height Z, half-width X)
    (PAD_T - 3.0, 17.35, 17.3),
    (157.6, 24.6, 23.0),
]

# serrated ring
RING_Y = 153.0
RING_L = 14.3
RING_A = 24.9           # half width (X)
RING_B = 26.8           # half height (Z)
TOOTH_D = 4.6
N_TEETH = 18

# flared oval collar
COL_L = 59.3
COL_A0, COL_B0 = 22.9, 25.5
COL_A1, COL_B1 = 24.7, 29.8

# square spindle stub
SP_L = 10.5
SP_W = 21.7
SP_H = 34.2

# screw head on the back of the pad with a raised bar across it
SCR_R = 18.0
SCR_C = (32.2, 25.0)    # (Y, Z) of the centre of its back face
SCR_TILT = 0.0         # degrees (positive = face turned upward)
SCR_T = 5.0
BAR_H = 8.0             # height of the raised bar across the head
BAR_P = 4.2             # protrusion of the bar beyond the head face
BAR_ARC_R = 29.0        # plan-view radius of the bar's back face
NECK_ZC = 4.5           # centre height of the neck section at the pad
NECK_A = 17.8           # neck half width at the pad
NECK_B = 21.3           # neck half height at the pad
NECK_Y1 = 46.0          # where the neck runs out into the shaft


def k(v):
    return v * K


def yplane(y):
    """Plane normal +Y at height y; local x = -Z (seam at the bottom), local y = -X."""
    return cq.Plane(origin=(0, k(y), 0), xDir=(0, 0, -1), normal=(0, 1, 0))


def oval(wp, b, a):
    """Ellipse with half-height b (Z) and half-width a (X); keep major axis on local x."""
    if b < a:
        b = a + 0.01
    return wp.ellipse(k(b), k(a))


def tangent_pts(c1, r1, c2, r2, side):
    dx, dz = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dz)
    ux, uz = dx / d, dz / d
    cth = (r1 - r2) / d
    sth = math.sqrt(1 - cth * cth)
    px, pz = -uz, ux
    if px * side < 0:
        px, pz = -px, -pz
    nx, nz = cth * ux + sth * px, cth * uz + sth * pz
    return (c1[0] + r1 * nx, c1[1] + r1 * nz), (c2[0] + r2 * nx, c2[1] + r2 * nz)


# ---------------- pad ----------------
CT = (k(PAD_XT), k(PAD_TOP - PAD_RT))
CB = (k(PAD_XB), k(PAD_BOT + PAD_RB))
p1r, p2r = tangent_pts(CT, k(PAD_RT), CB, k(PAD_RB), +1)
p1l, p2l = tangent_pts(CT, k(PAD_RT), CB, k(PAD_RB), -1)

pad_plane = cq.Plane(origin=(0, 0, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
egg = (
    cq.Workplane(pad_plane)
    .moveTo(*p1r)
    .threePointArc((CT[0], k(PAD_TOP)), p1l)
    .lineTo(*p2l)
    .threePointArc((CB[0], k(PAD_BOT)), p2r)
    .close()
    .extrude(-k(PAD_T + 4.0))
)
# slightly inclined back face: thicker at the bottom than at the top
side_pl = cq.Plane(origin=(-k(60), 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
zb_, zt_ = PAD_BOT - 10.0, PAD_TOP + 10.0
back_cut = (
    cq.Workplane(side_pl)
    .polyline(
        [
            (-k(1.0), k(zb_)),
            (k(PAD_T + PAD_BACK_TILT * (0.5 - (zb_ - PAD_BOT) / (PAD_TOP - PAD_BOT))), k(zb_)),
            (k(PAD_T + PAD_BACK_TILT * (0.5 - (zt_ - PAD_BOT) / (PAD_TOP - PAD_BOT))), k(zt_)),
            (-k(1.0), k(zt_)),
        ]
    )
    .close()
    .extrude(k(120))
)
egg = egg.intersect(back_cut)


def law(pairs):
    arr = TColgp_Array1OfPnt2d(1, len(pairs))
    for i, (u, r) in enumerate(pairs):
        arr.SetValue(i + 1, gp_Pnt2d(u, r))
    return arr


# variable radius rounding of the back edge: big at the top, small at the bottom
egg_s = egg.val()
back_face = max(egg.faces().vals(), key=lambda f: f.Center().y)
top_edge = max(back_face.Edges(), key=lambda e: e.Center().z)
mf = BRepFilletAPI_MakeFillet(egg_s.wrapped)
mf.Add(k(PAD_R_SIDE), top_edge.wrapped)
rt, rs, rl, rb = k(PAD_R_TOP), k(PAD_R_SIDE), k(PAD_R_LOW), k(PAD_R_BOT)
cont = [cq.Edge(mf.Edge(1, i)) for i in range(1, mf.NbEdges(1) + 1)]
i_top = max(range(len(cont)), key=lambda j: cont[j].Center().z)
i_bot = min(range(len(cont)), key=lambda j: cont[j].Center().z)
for j, e in enumerate(cont):
    u0, u1 = e._bounds()
    zs, ze = e.startPoint().z, e.endPoint().z
    if j == i_top:                                           # top arc
        du = u1 - u0
        rsh = rs + PAD_R_SHOULDER * (rt - rs)
        mf.SetRadius(
            law([(u0, rs), (u0 + 0.25 * du, rsh), (u0 + 0.5 * du, rt), (u0 + 0.75 * du, rsh), (u1, rs)]),
            1, j + 1,
        )
    elif j == i_bot:                                         # bottom arc
        mf.SetRadius(law([(u0, rl), (0.5 * (u0 + u1), rb), (u1, rl)]), 1, j + 1)
    else:                                                    # sides
        r_s = rs if zs > ze else rl
        r_e = rs if ze > zs else rl
        mf.SetRadius(r_s, r_e, 1, j + 1)
mf.Build()
pad = cq.Workplane().add(cq.Shape.cast(mf.Shape()))
pad = pad.faces("<Y").edges().fillet(k(PAD_R_FRONT))

# ---------------- shaft ----------------
y_prev = SH_SECTIONS[0][0]
sw = oval(cq.Workplane(yplane(y_prev)), SH_SECTIONS[0][1], SH_SECTIONS[0][2])
for y, b, a in SH_SECTIONS[1:]:
    sw = oval(sw.workplane(offset=k(y - y_prev)), b, a)
    y_prev = y
shaft = sw.loft(combine=True, ruled=True)

# ---------------- neck: the shaft rises into the screw head near the pad ----------------
def yplane_z(y, zc):
    return cq.Plane(origin=(0, k(y), k(zc)), xDir=(0, 0, -1), normal=(0, 1, 0))


def oval_wire(y, zc, b, a):
    if b < a:
        b = a + 0.01
    return cq.Workplane(yplane_z(y, zc)).ellipse(k(b), k(a)).val()


y0s, b0s, a0s = SH_SECTIONS[0]
y1s, b1s, a1s = SH_SECTIONS[-1]
fr = (NECK_Y1 - y0s) / (y1s - y0s)
nb = (b0s + fr * (b1s - b0s)) * 0.985
na = (a0s + fr * (a1s - a0s)) * 0.985
neck = cq.Workplane().add(
    cq.Solid.makeLoft(
        [oval_wire(PAD_T - 2.0, NECK_ZC, NECK_B, NECK_A), oval_wire(NECK_Y1, 0.0, nb, na)], True
    )
)

# ---------------- screw head (upper half visible) with a raised bar ----------------
tl = math.radians(SCR_TILT)
n_dir = (0.0, math.cos(tl), math.sin(tl))
scr_c = (0.0, k(SCR_C[0]), k(SCR_C[1]))
scr_plane = cq.Plane(origin=scr_c, xDir=(1, 0, 0), normal=n_dir)
head = cq.Workplane(scr_plane).circle(k(SCR_R)).extrude(-k(SCR_T))
head = head.intersect(
    cq.Workplane("XY").box(k(80), k(80), k(60), centered=(True, True, False))
    .translate((0, k(SCR_C[0]), k(SCR_C[1] - BAR_H / 2)))
)

bar = (
    cq.Workplane(scr_plane)
    .rect(k(2 * SCR_R + 2), k(BAR_H))
    .extrude(k(BAR_P + 6.0))
    .translate((0, -k(6.0) * n_dir[1], -k(6.0) * n_dir[2]))
)
bar = bar.intersect(
    cq.Workplane(scr_plane).circle(k(SCR_R + 1.0)).extrude(k(BAR_P + 7.0)).translate(
        (0, -k(6.0) * n_dir[1], -k(6.0) * n_dir[2])
    )
)
bar_arc = (
    cq.Workplane("XY")
    .workplane(offset=k(SCR_C[1] - 20))
    .center(0, k(SCR_C[0] + BAR_P - BAR_ARC_R))
    .circle(k(BAR_ARC_R))
    .extrude(k(40))
)
bar = bar.intersect(bar_arc)

neck = neck.union(shaft).union(head).union(bar)

# ---------------- ring with saw teeth ----------------
ring = oval(cq.Workplane(yplane(RING_Y)), RING_B, RING_A).extrude(k(RING_L))
ring = ring.faces(">Y").edges().fillet(k(1.6))

r_avg = k(0.5 * (RING_A + RING_B))
pitch = 2 * math.pi * r_avg / N_TEETH
ext = k(1.5)
td = k(TOOTH_D)
cutters = None
for i in range(N_TEETH):
    th = 2 * math.pi * i / N_TEETH
    u = (math.sin(th), 0.0, math.cos(th))
    t = (math.cos(th), 0.0, -math.sin(th))
    r0 = k(12.0)
    pl = cq.Plane(origin=(u[0] * r0, 0, u[2] * r0), xDir=t, normal=u)
    half = pitch / 2 * (td + ext) / td
    y0 = k(RING_Y)
    c = (
        cq.Workplane(pl)
        .polyline([(-half, y0 - ext), (half, y0 - ext), (0, y0 + td)])
        .close()
        .extrude(k(25.0))
    )
    cutters = c if cutters is None else cutters.union(c)
ring = ring.cut(cutters)

# ---------------- collar ----------------
col_y0 = RING_Y + RING_L - 0.5
collar = (
    oval(oval(cq.Workplane(yplane(col_y0)), COL_B0, COL_A0).workplane(offset=k(COL_L + 0.5)), COL_B1, COL_A1)
    .loft(combine=True, ruled=True)
)
col_end = col_y0 + COL_L + 0.5

# ---------------- spindle ----------------
spindle = (
    cq.Workplane(cq.Plane(origin=(0, k(col_end), 0), xDir=(1, 0, 0), normal=(0, 1, 0)))
    .rect(k(SP_W), k(SP_H))
    .extrude(k(SP_L))
    .edges("|Y").fillet(0.5)
)

result = pad.union(neck).union(ring).union(collar).union(spindle)
